import cadquery as cq

# ---- driving dimensions (mm) ----
FLANGE_D = 100.0      # flange outer diameter
FLANGE_T = 7.35       # flange thickness
BODY_D = 70.1         # cup outer diameter
TOTAL_H = 39.5        # flange bottom face to cup rim
BORE_D = 58.8         # cup bore diameter
FLOOR_T = FLANGE_T    # bore floor sits level with the flange top
HOLE_D = 8.1          # centre through hole in the floor
PIN_D = 3.6           # two dowel pins set into the bore wall at +Y / -Y
FOOT_D = 69.6         # thin foot under the cup on the bottom face
FOOT_T = 0.55
PIN_SINK = 0.03       # pin tops sit a hair below the rim face
SEAM_ANGLE = 90.0     # where the cylinder seams sit (towards the back)


def disc(d, h, z0=0.0):
    """Solid cylinder of diameter d, height h (may be negative) starting at z0,
    with its seam turned to SEAM_ANGLE."""
    return (cq.Workplane("XY")
            .transformed(offset=(0, 0, z0), rotate=(0, 0, SEAM_ANGLE))
            .circle(d / 2.0).extrude(h))


# ---- flanged cup ----
cup = disc(FLANGE_D, FLANGE_T).union(disc(BODY_D, TOTAL_H))   # flange + body
cup = cup.union(disc(FOOT_D, -FOOT_T))                         # thin foot below
cup = cup.cut(disc(BORE_D, TOTAL_H, FLOOR_T))                  # blind bore
cup = cup.cut(disc(HOLE_D, TOTAL_H + 2 * FOOT_T + 2, -FOOT_T - 1))  # centre hole

# ---- two dowel pins, axis on the bore surface, flush with the rim ----
pin_len = TOTAL_H - FLOOR_T - PIN_SINK
pins = [
    cq.Workplane("XY").workplane(offset=FLOOR_T)
    .center(0, sy * BORE_D / 2.0).circle(PIN_D / 2.0).extrude(pin_len)
    .val()
    for sy in (1, -1)
]

result = cq.Compound.makeCompound([cup.val()] + pins)
VIEW = {"azimuth": 45, "elevation": 26}
